import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# flange (obround-ish plate in XZ, thickness along Y)
FL_W = 60.0          # overall width (X)
FL_H = 30.0          # height (Z)
FL_T = 3.5           # thickness (Y)
FL_R = 13.0          # corner radius of flange ends

# housing block in front of flange
BX_W = 30.0          # X
BX_D = 10.0          # Y depth in front of flange
BX_H = FL_H          # Z (flush with flange top/bottom)

# main connector pocket in the block front face
PK_X0, PK_X1 = -11.6, 11.6
PK_Z0, PK_Z1 = -6.7, 11.7
PK_DEPTH = BX_D      # down to the flange face

# small lower pocket
SP_X0, SP_X1 = -7.4, 2.4
SP_Z0 = -13.3
SP_DEPTH = 2.5

# through holes in pocket floor
HOLE_D = 1.6
HOLE_PITCH = 4.15
HOLE_X_L, HOLE_X_R = -8.85, 8.75
HOLE_Z0 = -3.7
# tiny holes in the small pocket
TINY_D = 0.9
TINY_X = -5.0
TINY_Z = [-8.3, -10.0, -11.7]

# bosses and locating pins
BOSS_D = 11.6
BOSS_X = 20.75
PIN_D = 8.3
PIN_L = 16.5
PIN_TIP_R = 3.2

# mounting tab (vertical plate along +Y)
TAB_T = 3.4
TAB_L = 49.7
TAB_R = 12.5
TAB_ROOT_R = 4.5
TAB_HOLE_D = 11.8
TAB_HOLE_Y = 33.3
TAB_SMALL_D = 1.8
TAB_SMALL_Y = [21.7, 45.0]

# ---------------- build ----------------
y_front = -FL_T - BX_D  # front face of the block

# flange: y from -FL_T to 0
flange = (
    cq.Workplane("XZ")
    .rect(FL_W, FL_H)
    .extrude(FL_T)
    .edges("|Y")
    .fillet(FL_R)
)

# block in front of flange
block = (
    cq.Workplane("XY")
    .box(BX_W, BX_D, BX_H)
    .translate((0, -FL_T - BX_D / 2.0, 0))
)

# tab: x from -TAB_T/2..TAB_T/2, y from 0..TAB_L
tab = (
    cq.Workplane("YZ")
    .center(TAB_L / 2.0, 0)
    .rect(TAB_L, FL_H)
    .extrude(TAB_T / 2.0, both=True)
    .edges("|X and >Y")
    .fillet(TAB_R)
)

body = flange.union(block).union(tab)

# fillet the tab root (vertical edges where tab meets flange back face)
body = body.edges(
    cq.selectors.BoxSelector(
        (-TAB_T, -0.01, -FL_H), (TAB_T, 0.01, FL_H)
    )
).edges("|Z").fillet(TAB_ROOT_R)

# bosses + pins
for sx in (-1, 1):
    boss = (
        cq.Workplane("XZ", origin=(sx * BOSS_X, -FL_T, 0))
        .circle(BOSS_D / 2.0)
        .extrude(BX_D)
    )
    # pin with a generously rounded (blunt) tip
    pin = (
        cq.Workplane("XZ", origin=(sx * BOSS_X, y_front, 0))
        .circle(PIN_D / 2.0)
        .extrude(PIN_L)
        .faces("<Y")
        .edges()
        .fillet(PIN_TIP_R)
    )
    body = body.union(boss).union(pin)

# main pocket
pocket = (
    cq.Workplane("XY")
    .box(PK_X1 - PK_X0, PK_DEPTH, PK_Z1 - PK_Z0, centered=False)
    .translate((PK_X0, y_front, PK_Z0))
)
body = body.cut(pocket)

# small lower pocket (opens into the main pocket)
spocket = (
    cq.Workplane("XY")
    .box(SP_X1 - SP_X0, SP_DEPTH, PK_Z0 - SP_Z0 + 0.5, centered=False)
    .translate((SP_X0, y_front, SP_Z0))
)
body = body.cut(spocket)

# through holes along Y
hole_pts = [(HOLE_X_L, HOLE_Z0 + i * HOLE_PITCH) for i in range(4)]
hole_pts += [(HOLE_X_R, HOLE_Z0 + i * HOLE_PITCH) for i in range(2)]
holes = (
    cq.Workplane("XZ", origin=(0, 1.0, 0))
    .pushPoints(hole_pts)
    .circle(HOLE_D / 2.0)
    .extrude(FL_T + BX_D + 2.0)
)
body = body.cut(holes)

tiny = (
    cq.Workplane("XZ", origin=(0, 1.0, 0))
    .pushPoints([(TINY_X, z) for z in TINY_Z])
    .circle(TINY_D / 2.0)
    .extrude(FL_T + BX_D + 2.0)
)
body = body.cut(tiny)

# tab holes along X
tab_holes = (
    cq.Workplane("YZ", origin=(-TAB_T, 0, 0))
    .pushPoints([(TAB_HOLE_Y, 0)])
    .circle(TAB_HOLE_D / 2.0)
    .extrude(2 * TAB_T)
)
tab_small = (
    cq.Workplane("YZ", origin=(-TAB_T, 0, 0))
    .pushPoints([(y, 0) for y in TAB_SMALL_Y])
    .circle(TAB_SMALL_D / 2.0)
    .extrude(2 * TAB_T)
)
body = body.cut(tab_holes).cut(tab_small)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
